import math
import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
W = 100.0            # overall length along X (shaft axis)
Y_FRONT = -44.8      # front face (-Y)
Y_BACK = 43.2        # back face (+Y) of the right-hand portion
H = 40.0             # overall height; shaft axis lies on the top face
AXIS_Z = H

# walls (perpendicular to X)
LW_X0, LW_X1 = 0.0, 11.6      # left wall
MW_X0, MW_X1 = 44.8, 54.7     # middle wall
RW_X0, RW_X1 = 85.2, W        # right wall

# left portion: slanted back face
SLANT_Y0 = 21.0      # back face y at x = 0
SLANT_Y1 = 32.6      # back face y at x = MW_X0
R_SLANT_CONVEX = 6.0
R_SLANT_CONCAVE = 6.5
R_VERT = 1.0         # small rounds on the outer vertical corners
BOTTOM_CHAMFER = 0.5

# bays between the walls
LB_FLOOR = 24.6      # left bay floor height
LB_FILLET = 1.5
NOTCH_R = 1.2        # small rounds on the notch edges of the front face
FLOOR_BACK_R = 1.0   # round on the back edge of the left bay floor
RB_FLOOR = 15.7      # right bay floor height
RB_FILLET = 5.0
TROUGH_R = 43.2      # clearance trough in the right bay (coaxial with shaft)
TROUGH_FILLET = 1.0

# bearing cradles
R_LIP = 10.8         # shoulder / lip radius
R_SEAT = 12.2        # bearing seat radius
SEATS = [(2.15, 10.5), (45.7, 53.8), (86.3, 93.9)]

# holes
V_HOLE_D = 4.9       # vertical screw holes in the wall tops (through)
V_HOLE_Y = 16.1
V_HOLE_X = [5.8, 49.75, 90.1]
CB_D = 8.6           # counterbores for those holes on the underside
CB_DEPTH = 4.0
F_HOLE_D = 8.6       # horizontal bores in the front face (through along Y)
F_HOLE_Z = 14.6
F_HOLE_X = [15.5, 40.6]
F_CB_D = 13.0        # counterbores of those bores, from the slanted back face
F_CB_DEPTH = 9.0
B_HOLE_D = 7.0       # blind holes in the back face
B_HOLE_DEPTH = 8.0
B_HOLES = [(56.0, 7.7), (92.0, 7.3)]

# underside lightening pockets (mirror pair about the shaft plane)
POCKET_PTS = [(9.2, 5.4), (46.3, 5.4), (46.3, 8.6), (29.5, 20.2), (9.2, 10.0)]
POCKET_DEPTH = 6.5
POCKET_R = 1.4

# dish recess on the outer (+X) face of the right wall
DISH_R_OUT = 33.1   # rim radius on the face
DISH_R_FLAT = 25.4  # start of the flat annular floor
DISH_R_IN = 16.3    # end of the flat floor
DISH_R_RING = 13.4  # outer radius of the raised ring round the cradle
DISH_DEPTH = 4.0
BOSS_DEPTH = 2.3     # depth of the raised ring face below the outer face

# mouse-ear feet
FOOT_D = 11.4
FOOT_Z0, FOOT_Z1 = -0.1, 1.4
FOOT_DX, FOOT_DY = 3.0, 4.1   # offset of the ear centres from the body corners

# ---------------- helpers ----------------

def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def cyl_x(r, x0, x1, y=0.0, z=AXIS_Z):
    return (cq.Workplane("YZ").workplane(offset=x0)
            .center(y, z).circle(r).extrude(x1 - x0))


def cyl_y(r, y0, y1, x, z):
    return (cq.Workplane("XZ").workplane(offset=-y1)
            .center(x, z).circle(r).extrude(y1 - y0))


def cyl_z(r, z0, z1, x, y):
    return (cq.Workplane("XY").workplane(offset=z0)
            .center(x, y).circle(r).extrude(z1 - z0))


def slant_y(x):
    return SLANT_Y0 + (SLANT_Y1 - SLANT_Y0) * x / MW_X0


def near_edge(x, y, tol=0.1):
    return cq.selectors.BoxSelector((x - tol, y - tol, -5), (x + tol, y + tol, H + 5))


def arc_mid(c, p0, p1):
    a0 = math.atan2(p0[1] - c[1], p0[0] - c[0])
    a1 = math.atan2(p1[1] - c[1], p1[0] - c[0])
    da = a1 - a0
    while da > math.pi:
        da -= 2 * math.pi
    while da < -math.pi:
        da += 2 * math.pi
    r = math.hypot(p0[0] - c[0], p0[1] - c[1])
    am = a0 + da / 2
    return (c[0] + r * math.cos(am), c[1] + r * math.sin(am))


# ---------------- base block ----------------
outline = [
    (0.0, Y_FRONT), (W, Y_FRONT), (W, Y_BACK), (MW_X0, Y_BACK),
    (MW_X0, SLANT_Y1), (0.0, SLANT_Y0),
]
body = cq.Workplane("XY").polyline(outline).close().extrude(H)
body = body.edges(near_edge(MW_X0, SLANT_Y1)).fillet(R_SLANT_CONCAVE)
body = body.edges(near_edge(0.0, SLANT_Y0)).fillet(R_SLANT_CONVEX)
for (cx, cy) in [(0.0, Y_FRONT), (W, Y_FRONT), (W, Y_BACK), (MW_X0, Y_BACK)]:
    body = body.edges(near_edge(cx, cy)).fillet(R_VERT)
# small chamfer round the bottom perimeter
body = body.faces("<Z").edges().chamfer(BOTTOM_CHAMFER)

# ---------------- bays ----------------
lb = (box(LW_X1, MW_X0, Y_FRONT - 20, Y_BACK + 20, LB_FLOOR, H + 20)
      .edges("|Y and <Z").fillet(LB_FILLET))
rb = (box(MW_X1, RW_X0, Y_FRONT - 20, Y_BACK + 20, RB_FLOOR, H + 20)
      .edges("|Y and <Z").fillet(RB_FILLET))
# clearance trough (coaxial with the shaft) -> opens a window in the base
trough = cyl_x(TROUGH_R, MW_X1, RW_X0)
body = body.cut(lb.union(rb).union(trough))


def _trough_edge(e):
    # intersection arcs of the trough with the two wall faces
    bb = e.BoundingBox()
    if e.geomType() != "CIRCLE":
        return False
    for xw in (MW_X1, RW_X0):
        if abs(bb.xmin - xw) < 0.01 and abs(bb.xmax - xw) < 0.01:
            return abs(e.radius() - TROUGH_R) < 0.01
    return False


body = body.newObject([e for e in body.edges().vals() if _trough_edge(e)]).fillet(TROUGH_FILLET)

# soften the left bay notch edges on the front face and the back edge of its floor
def _front_notch_edge(e):
    bb = e.BoundingBox()
    c = e.Center()
    return (bb.ymin > Y_FRONT - 0.01 and bb.ymax < Y_FRONT + 0.01
            and bb.xmin > LW_X1 - 0.01 and bb.xmax < MW_X0 + 0.01 and 0.5 < c.z < H - 0.05)


def _floor_back_edge(e):
    bb = e.BoundingBox()
    c = e.Center()
    return (abs(c.z - LB_FLOOR) < 0.01 and bb.zmax - bb.zmin < 0.01
            and c.y > 10.0 and c.x < MW_X0)


body = body.newObject([e for e in body.edges().vals() if _front_notch_edge(e)]).fillet(NOTCH_R)
body = body.newObject([e for e in body.edges().vals() if _floor_back_edge(e)]).fillet(FLOOR_BACK_R)

# ---------------- bearing cradles ----------------
cradle = cyl_x(R_LIP, -5, W + 5)
for (x0, x1) in SEATS:
    cradle = cradle.union(cyl_x(R_SEAT, x0, x1))
body = body.cut(cradle)

# ---------------- dish recess on the +X face ----------------
# profile in the (x, r) half plane, revolved about the shaft axis:
# concave arc from the rim down to a flat annular floor, then a concave
# arc rising to a raised ring around the cradle
L_OUT = DISH_R_OUT - DISH_R_FLAT
rho_o = (DISH_DEPTH ** 2 + L_OUT ** 2) / (2 * DISH_DEPTH)
L_IN = DISH_R_IN - DISH_R_RING
STEP = DISH_DEPTH - BOSS_DEPTH
rho_i = (STEP ** 2 + L_IN ** 2) / (2 * STEP)
p_rim = (W, DISH_R_OUT)
p_bot_o = (W - DISH_DEPTH, DISH_R_FLAT)
p_bot_i = (W - DISH_DEPTH, DISH_R_IN)
p_ring = (W - BOSS_DEPTH, DISH_R_RING)
c_o = (W - DISH_DEPTH + rho_o, DISH_R_FLAT)
c_i = (W - DISH_DEPTH + rho_i, DISH_R_IN)
prof = (cq.Workplane("XY")
        .moveTo(W + 1.0, 0.0)
        .lineTo(W + 1.0, DISH_R_OUT)
        .lineTo(*p_rim)
        .threePointArc(arc_mid(c_o, p_rim, p_bot_o), p_bot_o)
        .lineTo(*p_bot_i)
        .threePointArc(arc_mid(c_i, p_bot_i, p_ring), p_ring)
        .lineTo(W - BOSS_DEPTH, 0.0)
        .close())
dish = prof.revolve(360, (0, 0, 0), (1, 0, 0)).translate((0, 0, AXIS_Z))
body = body.cut(dish)

# ---------------- holes ----------------
tools = []
for x in V_HOLE_X:
    for y in (-V_HOLE_Y, V_HOLE_Y):
        tools.append(cyl_z(V_HOLE_D / 2, -5, H + 5, x, y))
        tools.append(cyl_z(CB_D / 2, -5, CB_DEPTH, x, y))
for x in F_HOLE_X:
    tools.append(cyl_y(F_HOLE_D / 2, Y_FRONT - 5, Y_BACK + 5, x, F_HOLE_Z))
    tools.append(cyl_y(F_CB_D / 2, slant_y(x) - F_CB_DEPTH, Y_BACK + 5, x, F_HOLE_Z))
for (x, z) in B_HOLES:
    tools.append(cyl_y(B_HOLE_D / 2, Y_BACK - B_HOLE_DEPTH, Y_BACK + 5, x, z))
body = cq.Workplane("XY").newObject([body.val().cut(*[t.val() for t in tools]).clean()])

# ---------------- underside pockets ----------------
pockets = []
for sgn in (1, -1):
    pts = [(x, sgn * y) for (x, y) in POCKET_PTS]
    sk = cq.Sketch().polygon(pts + [pts[0]]).vertices().fillet(POCKET_R)
    pockets.append(cq.Workplane("XY").workplane(offset=-1.0).placeSketch(sk)
                   .extrude(POCKET_DEPTH + 1.0).val())
body = cq.Workplane("XY").newObject([body.val().cut(*pockets).clean()])

# ---------------- mouse-ear feet ----------------
dx, dy = FOOT_DX, FOOT_DY
feet = [
    (0.0 - dx, Y_FRONT - dy),
    (W + dx, Y_FRONT - dy),
    (W + dx, Y_BACK + dy),
    (MW_X0 - dx, Y_BACK + dy),
    (0.0 - 2.4, SLANT_Y0 + 2.0),
]
ears = (cq.Workplane("XY").workplane(offset=FOOT_Z0)
        .pushPoints(feet).circle(FOOT_D / 2).extrude(FOOT_Z1 - FOOT_Z0))
body = body.union(ears)

result = body
